import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_CENTER = 24.7      # radius of the central lobe of the flange outline
R_END = 8.9          # radius of the two end lobes (also radius of the end domes)
END_OFFSET = 44.1    # distance from the centre to the end-lobe centres (along Y)
T = 13.8             # flange thickness (along X)
BORE_D = 30.0        # central through bore
BOSS_BASE_R = 23.4   # base radius of the (about 45 deg) conical boss on the back face
BOSS_H = 8.2         # boss height; the cone runs out exactly at the bore edge
DOME_CYL = 2.0       # straight cylindrical length of the end domes behind the back face
SIDE_HOLE_D = 9.0    # radial cross hole from the bottom edge into the bore

VIEW = {"azimuth": 45, "elevation": 26}

bore_r = BORE_D / 2.0
boss_h = BOSS_H
slope = (BOSS_BASE_R - bore_r) / boss_h   # radial drop per mm of height

# ---------------- flange outline (YZ plane), extruded along +X ----------------
s = (R_CENTER - R_END) / END_OFFSET      # sine of the tangent-line inclination
c = math.sqrt(1.0 - s * s)

outline = (
    cq.Workplane("YZ")
    .moveTo(R_CENTER * s, R_CENTER * c)
    .lineTo(END_OFFSET + R_END * s, R_END * c)
    .threePointArc((END_OFFSET + R_END, 0), (END_OFFSET + R_END * s, -R_END * c))
    .lineTo(R_CENTER * s, -R_CENTER * c)
    .threePointArc((0, -R_CENTER), (-R_CENTER * s, -R_CENTER * c))
    .lineTo(-END_OFFSET - R_END * s, -R_END * c)
    .threePointArc((-END_OFFSET - R_END, 0), (-END_OFFSET - R_END * s, R_END * c))
    .lineTo(-R_CENTER * s, R_CENTER * c)
    .threePointArc((0, R_CENTER), (R_CENTER * s, R_CENTER * c))
    .close()
)
plate = outline.extrude(T)  # back face at x = 0, front face at x = T


# ---------------- end lobes: cylinder coaxial with the end arcs + hemispherical dome ----------------
def end_lobe(x_start):
    """Revolved lobe at the -Y end: cylinder R_END from x_start back to -DOME_CYL, hemisphere cap."""
    k = math.sqrt(0.5)
    return (
        cq.Workplane("XZ", origin=(0, -END_OFFSET, 0))  # local x = X, local y = Z
        .moveTo(x_start, 0)
        .lineTo(x_start, R_END)
        .lineTo(-DOME_CYL, R_END)
        .threePointArc((-DOME_CYL - R_END * k, R_END * k), (-DOME_CYL - R_END, 0))
        .close()
        .revolve(360, (0, 0, 0), (1, 0, 0))
    )


# preferred: lobe cylinder runs through the flange so it merges with the end arcs into one face
lobe = end_lobe(T)
part = plate.union(lobe).union(lobe.mirror("XZ")).clean()
if not part.val().isValid():
    # fallback: lobes start on the back face
    lobe = end_lobe(0.0)
    part = plate.union(lobe).union(lobe.mirror("XZ")).clean()

# ---------------- conical boss around the bore on the back face ----------------
e = 1.0  # cone is run past the bore edge; the bore cut trims it exactly at x = -boss_h
boss = (
    cq.Workplane("XY")
    .polyline([(0, 0), (0, BOSS_BASE_R),
               (-(boss_h + e), bore_r - e * slope),
               (-(boss_h + e), 0)])
    .close()
    .revolve(360, (0, 0, 0), (1, 0, 0))
)
part = part.union(boss)

# ---------------- central through bore ----------------
bore = (
    cq.Workplane("YZ", origin=(-boss_h - 2, 0, 0))
    .transformed(rotate=(0, 0, 90))       # put the cylinder seam on top
    .circle(bore_r)
    .extrude(T + boss_h + 4)
)
part = part.cut(bore)

# ---------------- radial cross hole from the bottom edge into the bore ----------------
side = (
    cq.Workplane("XY", origin=(T / 2.0, 0, -R_CENTER - 2))
    .circle(SIDE_HOLE_D / 2.0)
    .extrude(R_CENTER + 2 - bore_r * 0.5)
)
part = part.cut(side)

result = part.clean()
